import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
R_OUT = 50.0          # ring outer radius
T_RING = 2.0          # ring radial wall
W_RING = 24.2         # ring width along X
GAP = 1.5             # split gap at top / bottom
T_WEB = 2.0           # central web thickness (at X = 0)
T_RIB = 2.0           # horizontal rib thickness (at Z = 0)
T_PLATE = 2.0         # side plate thickness
INNER_HX = 6.4        # half width (X) of the inner plates / ribs
COL_HALF = 20.3       # half width of the central opening (Y)
POCKET_R = 2.0        # pocket corner radius
FLOOR_F = 1.4         # pocket floor fillet
LR_F = 2.5            # plate-to-ring fillet under the right lobe
COL_R = 5.5           # central opening corner radius

# notch (keyhole) in ring near the split
NOTCH_Y = 12.0
NOTCH_X = -7.4
NOTCH_D = 7.6
NECK_W = 4.0
LIP_R = 1.0           # rounding of the notch mouth
END_R = 1.8           # rounding of ring-end corners

# servo-like boxes
BOX_L = 55.5          # long side
BOX_W = 2 * COL_HALF  # along Y
BOX_H = 43.3          # height
BOX_F = 2.0           # fillet of the edges round the +/-Y faces
HORN_OFF = 12.0       # horn centre from box end
HORN_D = 24.0
HORN_T = 2.7

LEFT_X0 = -59.0       # left box outer end
RIGHT_X1 = 43.2       # right box outer end
RIGHT_Z1 = 11.9       # right box top

# side plates (lobes) with hole pattern
LOBE_L_X0 = -40.0
LOBE_R_Z1 = -6.9
LOBE_RAD_L = 11.5
LOBE_RAD_R = 10.0
LOBE_CONC = 5.5       # concave junction radius
HOLE_C_D = 9.6
HOLE_S_D = 2.4
HOLE_S_P = 11.8       # small hole pitch
HOLE_L_X = -21.6      # hole pattern centre on the left lobe (Z = 0)
HOLE_R_X = 21.5       # hole pattern centre on the right lobe (Z = lobe centre)

R_IN = R_OUT - T_RING
HX = W_RING / 2.0

# ---------------- ring band ----------------
ring = (cq.Workplane("YZ").workplane(offset=-HX)
        .circle(R_OUT).circle(R_IN).extrude(W_RING))

# ---------------- inner web: plates, ribs, thin centre web ----------------
inner = (cq.Workplane("YZ").workplane(offset=-INNER_HX)
         .circle(R_IN + 0.5).extrude(2 * INNER_HX))

col = (cq.Sketch()
       .circle(R_IN)
       .rect(2 * COL_HALF, 4 * R_OUT, mode="i")
       .vertices().fillet(COL_R))
col_cut = (cq.Workplane("YZ").workplane(offset=-HX - 1)
           .placeSketch(col).extrude(W_RING + 2))
inner = inner.cut(col_cut)

y0 = COL_HALF + T_PLATE
z0 = T_RIB / 2.0
for sy in (1, -1):
    for sz in (1, -1):
        cy = sy * (y0 + R_OUT) / 2.0
        cz = sz * (z0 + R_OUT) / 2.0
        sk = (cq.Sketch()
              .circle(R_IN)
              .push([(cy, cz)])
              .rect(R_OUT - y0, R_OUT - z0, mode="i")
              .reset()
              .vertices().fillet(POCKET_R))
        for sx in (1, -1):
            if sx > 0:
                wp = cq.Workplane("YZ").workplane(offset=T_WEB / 2.0)
            else:
                wp = cq.Workplane("YZ").workplane(offset=-INNER_HX - 1)
            pk = wp.placeSketch(sk).extrude(INNER_HX - T_WEB / 2.0 + 1)
            inner = inner.cut(pk)

# small fillet round the pocket floors
_f1 = cq.selectors.BoxSelector((T_WEB / 2 - 0.05, -60, -60), (T_WEB / 2 + 0.05, 60, 60))
_f2 = cq.selectors.BoxSelector((-T_WEB / 2 - 0.05, -60, -60), (-T_WEB / 2 + 0.05, 60, 60))
inner = inner.edges(_f1 + _f2).fillet(FLOOR_F)

hub = ring.union(inner)

# fillet between the lower side-plate faces and the ring (full ring width on +X)
_yw = COL_HALF + T_PLATE
_yc = -(_yw + LR_F)
_zc = -math.sqrt((R_IN - LR_F) ** 2 - _yc ** 2)
_ty = _yc * R_IN / (R_IN - LR_F)
_zl = -R_IN - 1.0
wsk = (cq.Sketch()
       .push([((_ty + -_yw) / 2.0, (_zl + _zc) / 2.0)])
       .rect(-_yw - _ty, _zc - _zl)
       .reset()
       .circle(R_IN + 0.3, mode="i")
       .reset()
       .push([(_yc, _zc)]).circle(LR_F, mode="s")
       .reset())
wedge = (cq.Workplane("YZ").workplane(offset=T_WEB / 2.0)
         .placeSketch(wsk).extrude(HX - T_WEB / 2.0))
hub = hub.union(wedge).union(wedge.mirror("XZ"))

# split gaps top and bottom
for sz in (1, -1):
    g = cq.Workplane("XY").box(W_RING + 2, GAP, 12).translate((0, 0, sz * R_OUT))
    hub = hub.cut(g)

# round the corners of the ring ends at the splits
_gsel = None
for sx in (1, -1):
    for sy in (1, -1):
        for sz in (1, -1):
            c = (sx * HX, sy * GAP / 2.0, sz * (R_OUT - T_RING / 2.0))
            b = cq.selectors.BoxSelector((c[0] - 0.2, c[1] - 0.2, c[2] - 1.5),
                                         (c[0] + 0.2, c[1] + 0.2, c[2] + 1.5))
            _gsel = b if _gsel is None else _gsel + b
hub = hub.edges(_gsel).fillet(END_R)

# keyhole notches on the -X edge near each split
def _rotx(p, a_deg):
    a = math.radians(a_deg)
    return (p[0], p[1] * math.cos(a) - p[2] * math.sin(a),
            p[1] * math.sin(a) + p[2] * math.cos(a))


theta = math.degrees(math.asin(NOTCH_Y / R_OUT))
neck_len = NOTCH_X + HX + 2.0
_lsel = None
for sz in (1, -1):
    for sy in (1, -1):
        ksk = (cq.Sketch()
               .push([(NOTCH_X, 0)]).circle(NOTCH_D / 2.0)
               .reset()
               .push([(NOTCH_X - neck_len / 2.0, 0)])
               .rect(neck_len, NECK_W)
               .reset())
        cutter = (cq.Workplane("XY").workplane(offset=R_OUT - 6)
                  .placeSketch(ksk).extrude(10))
        cutter = cutter.rotate((0, 0, 0), (1, 0, 0), -sy * theta)
        if sz < 0:
            cutter = cutter.rotate((0, 0, 0), (1, 0, 0), 180)
        hub = hub.cut(cutter)
        for sw in (1, -1):
            p = _rotx((-HX, sw * NECK_W / 2.0, R_OUT - T_RING / 2.0), -sy * theta)
            if sz < 0:
                p = _rotx(p, 180)
            b = cq.selectors.BoxSelector((p[0] - 0.3, p[1] - 0.6, p[2] - 0.6),
                                         (p[0] + 0.3, p[1] + 0.6, p[2] + 0.6))
            _lsel = b if _lsel is None else _lsel + b
hub = hub.edges(_lsel).fillet(LIP_R)

# ---------------- boxes ----------------
def box_shape(dx, dy, dz):
    return cq.Workplane("XY").box(dx, dy, dz).edges("|X or |Z").fillet(BOX_F)

# left box: long axis X, horn discs on top / bottom
lb_cx = LEFT_X0 + BOX_L / 2.0
left_box = box_shape(BOX_L, BOX_W, BOX_H).translate((lb_cx, 0, 0))
hx = LEFT_X0 + HORN_OFF
for sz in (1, -1):
    d = (cq.Workplane("XY").circle(HORN_D / 2.0).extrude(HORN_T + 0.5)
         .translate((hx, 0, BOX_H / 2.0 - 0.5)))
    if sz < 0:
        d = d.mirror("XY")
    left_box = left_box.union(d)

# right box: long axis Z, horn discs on +X / -X faces
rb_cz = RIGHT_Z1 - BOX_L / 2.0
rb_cx = RIGHT_X1 - BOX_H / 2.0
right_box = box_shape(BOX_H, BOX_W, BOX_L).translate((rb_cx, 0, rb_cz))
hz = RIGHT_Z1 - HORN_OFF
for sx in (1, -1):
    d = (cq.Workplane("YZ").circle(HORN_D / 2.0).extrude(HORN_T + 0.5)
         .translate((-0.5, 0, 0)))
    if sx > 0:
        d = d.translate((RIGHT_X1, 0, hz))
    else:
        d = d.mirror("YZ").translate((RIGHT_X1 - BOX_H, 0, hz))
    right_box = right_box.union(d)

# ---------------- side plates (strip in ring + two lobes) ----------------
ZB = RIGHT_Z1 - BOX_L          # bottom of right box / right lobe
ZT = -ZB                       # top of strip (buried in ring)
LZ = BOX_H / 2.0
outline = [
    (-INNER_HX, ZT), (-INNER_HX, LZ), (LOBE_L_X0, LZ), (LOBE_L_X0, -LZ),
    (-INNER_HX, -LZ), (-INNER_HX, ZB), (RIGHT_X1, ZB), (RIGHT_X1, LOBE_R_Z1),
    (INNER_HX, LOBE_R_Z1), (INNER_HX, ZT),
]


def corner_sel(x, z):
    return cq.selectors.BoxSelector((x - 0.3, -100, z - 0.3), (x + 0.3, 100, z + 0.3))


hole_l = (HOLE_L_X, 0.0)
hole_r = (HOLE_R_X, (ZB + LOBE_R_Z1) / 2.0)

plate = (cq.Workplane("XZ").polyline(outline).close().extrude(-T_PLATE))
for (x, z, rad) in [
        (LOBE_L_X0, LZ, LOBE_RAD_L), (LOBE_L_X0, -LZ, LOBE_RAD_L),
        (RIGHT_X1, ZB, LOBE_RAD_R), (RIGHT_X1, LOBE_R_Z1, LOBE_RAD_R),
        (-INNER_HX, LZ, LOBE_CONC), (-INNER_HX, -LZ, LOBE_CONC),
        (INNER_HX, LOBE_R_Z1, LOBE_CONC)]:
    plate = plate.edges(corner_sel(x, z)).fillet(rad)

for hc in (hole_l, hole_r):
    pts = [(hc[0] + i * HOLE_S_P / 2.0, hc[1] + j * HOLE_S_P / 2.0)
           for i in (-1, 1) for j in (-1, 1)]
    hcut = (cq.Workplane("XZ").workplane(offset=-T_PLATE - 1)
            .center(hc[0], hc[1]).circle(HOLE_C_D / 2.0).extrude(T_PLATE + 2))
    scut = (cq.Workplane("XZ").workplane(offset=-T_PLATE - 1)
            .pushPoints(pts).circle(HOLE_S_D / 2.0).extrude(T_PLATE + 2))
    plate = plate.cut(hcut).cut(scut)

plate_back = plate.translate((0, COL_HALF, 0))
plate_front = plate_back.mirror("XZ")

result = (hub.union(left_box).union(right_box)
          .union(plate_back).union(plate_front).clean())
